import math
import cadquery as cq

# ============ driving dimensions (mm) ============
OD = 70.0            # outer diameter of the ring
H = 16.2             # overall height
HOLE_D = 40.0        # through hole in the top plate
TOP_T = 4.4          # thickness of the top plate (shoulder at H - TOP_T)

BORE_D = 61.0        # counterbore from below (wall between the thread turns)

# internal closure thread: a single right-hand helical rib on the bore wall
RIB_D = 56.0         # inner (crest) diameter of the rib
RIB_P = 7.4          # pitch
RIB_CREST_W = 1.75   # axial width of the flat crest
RIB_FLANK_H = 2.0    # axial length of each flank
RIB_PHASE_Z = 1.0    # height of the rib centre at azimuth RIB_PHASE_A
RIB_PHASE_A = 135.0  # (deg) azimuth where RIB_PHASE_Z is defined

TG_R = 32.2          # mean radius of the small shallow groove in the top face
TG_W = 0.5           # width of that groove
TG_D = 0.15          # depth of that groove

SEAM_A = 186.0       # (deg) azimuth of the seam of the revolved faces

# ============ derived values ============
R = OD / 2.0
r_hole = HOLE_D / 2.0
z_sh = H - TOP_T
r_bore = BORE_D / 2.0
r_rib = RIB_D / 2.0

# ============ ring body: revolved half cross-section (x = radius, z = height) ============
outline = [
    (r_bore, 0.0),
    (R, 0.0),
    (R, H),
    (TG_R + TG_W / 2.0, H),
    (TG_R + TG_W / 2.0, H - TG_D),
    (TG_R - TG_W / 2.0, H - TG_D),
    (TG_R - TG_W / 2.0, H),
    (r_hole, H),
    (r_hole, z_sh),
    (r_bore, z_sh),
]
body = (cq.Workplane("XZ").polyline(outline).close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_A))


# ============ thread rib ============
def rib_profile_pts(zc, r_out):
    """Trapezoidal rib section centred at height zc, from the crest out to r_out."""
    k = RIB_FLANK_H / (r_bore - r_rib)          # axial growth per mm of radius
    hc = RIB_CREST_W / 2.0
    hb = hc + k * (r_out - r_rib)
    return [(r_out, zc - hb), (r_rib, zc - hc), (r_rib, zc + hc), (r_out, zc + hb)]


def helical_rib():
    ov = 0.4                                      # overlap into the wall
    z_start = RIB_PHASE_Z - RIB_P * RIB_PHASE_A / 360.0 - RIB_P   # rib centre at azimuth 0
    length = z_sh - z_start + RIB_P
    sec = cq.Workplane("XZ").polyline(rib_profile_pts(z_start, r_bore + ov)).close()
    path = cq.Wire.makeHelix(pitch=RIB_P, height=length, radius=r_bore + ov,
                             center=cq.Vector(0, 0, z_start), lefthand=False)
    rib = cq.Solid.sweep(sec.wires().val(), [], path, makeSolid=True, isFrenet=True)
    window = cq.Solid.makeBox(2 * R, 2 * R, z_sh, cq.Vector(-R, -R, 0))
    rib = rib.intersect(window)
    return body.union(cq.Workplane("XY").add(rib))


def ring_ribs():
    """Fallback: the same rib as plain revolved rings (no helix)."""
    res = body
    zc = RIB_PHASE_Z
    while zc - RIB_P > -RIB_P:
        zc -= RIB_P
    while zc < z_sh + RIB_P:
        ring = (cq.Workplane("XZ").polyline(rib_profile_pts(zc, r_bore + 0.4)).close()
                .revolve(360.0, (0, 0, 0), (0, 1, 0)))
        res = res.union(ring)
        zc += RIB_P
    clip = cq.Workplane("XY").circle(R + 1).extrude(H)
    return res.intersect(clip)


try:
    result = helical_rib()
    if not result.val().isValid() or len(result.solids().vals()) != 1:
        raise ValueError("bad helical rib")
except Exception:
    result = ring_ribs()

VIEW = {"azimuth": 45, "elevation": 26}
